import cadquery as cq
import math

# Socket-weld style flange: round flange plate with a filleted hub on top,
# a socket (counterbore) from the hub top down to the flange level, a
# smaller through bore, and four chamfered bolt holes.

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 100.0         # flange outer diameter
FLANGE_T = 7.6           # flange thickness
FLANGE_CHAMFER = 1.25    # chamfer on top outer edge of flange

HUB_D = 47.6             # hub outer diameter
TOTAL_H = 32.5           # overall height (flange bottom to hub top)
HUB_FILLET = 12.6        # fillet radius between hub and flange top
HUB_TOP_CHAMFER = 1.2    # outer chamfer at hub top
BORE_TOP_CHAMFER = 1.25  # inner chamfer at socket mouth

SOCKET_D = 37.6          # socket (counterbore) diameter, from hub top
SOCKET_FLOOR = FLANGE_T  # socket floor height above flange bottom
BORE_D = 25.0            # through bore diameter

BOLT_N = 4               # bolt holes, first one on +X
BOLT_PCD = 84.4
BOLT_D = 10.0
BOLT_CHAMFER = 0.6       # 45 deg chamfer at top of each bolt hole

# angular position of the (invisible-in-reality) seam lines of the
# revolved faces -- parked where the main view does not see them
OUTER_SEAM = 135.0
INNER_SEAM = -45.0

# ---------------- derived ----------------
FR = FLANGE_D / 2
HR = HUB_D / 2
SR = SOCKET_D / 2
BR = BORE_D / 2
T = FLANGE_T
H = TOTAL_H
F = HUB_FILLET
k = 1.0 - math.sqrt(0.5)   # 45 deg point of the fillet arc
c1 = FLANGE_CHAMFER
c2 = HUB_TOP_CHAMFER
c3 = BORE_TOP_CHAMFER
ZS = SOCKET_FLOOR


def revolve_z(wp, seam_deg):
    """revolve an XZ-plane (r, z) profile a full turn about the Z axis"""
    return wp.revolve(360, (0, 0, 0), (0, 1, 0)).rotate(
        (0, 0, 0), (0, 0, 1), seam_deg
    )


# ---------------- outer body: flange + filleted hub ----------------
outer_profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(FR, 0)
    .lineTo(FR, T - c1)                      # flange rim
    .lineTo(FR - c1, T)                      # flange top chamfer
    .lineTo(HR + F, T)                       # flange top face
    .threePointArc((HR + F * k, T + F * k), (HR, T + F))   # hub fillet
    .lineTo(HR, H - c2)                      # hub wall
    .lineTo(HR - c2, H)                      # hub top chamfer
    .lineTo(0, H)                            # hub top face
    .close()
)
body = revolve_z(outer_profile, OUTER_SEAM)

# ---------------- socket + through bore ----------------
bore_profile = (
    cq.Workplane("XZ")
    .moveTo(0, -1.0)
    .lineTo(BR, -1.0)
    .lineTo(BR, ZS)                          # through bore
    .lineTo(SR, ZS)                          # socket floor
    .lineTo(SR, H - c3)                      # socket wall
    .lineTo(SR + c3 + 1.0, H + 1.0)          # mouth chamfer (45 deg)
    .lineTo(0, H + 1.0)
    .close()
)
body = body.cut(revolve_z(bore_profile, INNER_SEAM))

# ---------------- bolt holes (with top chamfer) ----------------
BHR = BOLT_D / 2
bolt_cutter = revolve_z(
    cq.Workplane("XZ")
    .moveTo(0, -1.0)
    .lineTo(BHR, -1.0)
    .lineTo(BHR, T - BOLT_CHAMFER)
    .lineTo(BHR + BOLT_CHAMFER + 1.0, T + 1.0)
    .lineTo(0, T + 1.0)
    .close(),
    INNER_SEAM,
)
for i in range(BOLT_N):
    a = 2 * math.pi * i / BOLT_N
    x = BOLT_PCD / 2 * math.cos(a)
    y = BOLT_PCD / 2 * math.sin(a)
    body = body.cut(bolt_cutter.translate((x, y, 0)))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
